import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 34.0            # plate width (X)
R = W / 2.0         # end radius
LC = 42.35          # distance of end centres from origin (Y)
Z_TOP = 18.35       # top face of the plates

# -Y end (clevis with bore in lower plate)
A_TOP_BOT = 11.75   # underside of upper plate
A_STEP_Z = 9.3      # underside of the thickened root of the upper plate
A_STEP_Y = -36.9
A_BOT_TOP = -7.2    # upper face of lower plate
A_BOT_BOT = -18.3   # underside of lower plate
A_BORE_R = 9.0
A_KEY_W = 6.0
A_KEY_ANG = -45.0   # direction of the keyway slot (deg from +X)
A_CUP_R = 14.4      # circular recess in the upper plate
A_CUP_D = 3.0
A_POCKET_D = 5.0    # rounded pocket towards the body
A_SLOT_Y0 = -39.2   # rounded slot through the upper plate
A_SLOT_L = 18.0
A_SLOT_W = 6.4
A_SLOT_RC = 2.0
A_REC_R = 15.5      # annular recess under the lower plate
A_BOSS_R = 10.8
A_REC_TOP = -12.7
A_NOTCH_Y0, A_NOTCH_Y1 = -36.2, -27.7   # notch under the root of the lower plate
A_NOTCH_X = 12.0

# +Y end (hub end)
B_TOP_BOT = 7.85
B_BOT_TOP = -7.7
B_BOT_BOT = -15.0
HUB_R = 11.75
HUB_BORE = 9.4
HUB_GROOVE_Z = 0.0
B_CUP_R = 13.8
B_CUP_R2 = 14.6
B_NOTCH_X = 8.0

BODY_Y0 = -28.9     # body face in the -Y gap
BODY_Y1 = 31.6      # body face in the +Y gap

# raised rounded cover (top & bottom)
CAP_Y0, CAP_Y1 = -22.2, 24.2
CAP_H_TOP = 5.45    # rise above the plate top
CAP_H_BOT = 5.45    # drop below the lower plate
CAP_R1 = 4.4        # radius of the rounded long edges of the cover (lower part)
CAP_XM = 10.0       # the flat crown of the cover starts this far in from the side
CAP_R_END = 2.5

# side panel on -X
PANEL_T = 1.5
PANEL_Y0, PANEL_Y1 = -26.1, 30.3
PANEL_Z = 17.5
PANEL_CH0 = 4.0     # corner chamfer at the -Y end
PANEL_CH1 = 7.0     # corner chamfer at the +Y end

# inner channel through the body
CH_X0, CH_X1 = -9.3, 15.3
CH_Z0, CH_Z1 = -7.2, 10.5
CH_END_T = 2.0      # wall between the wide channel and the +Y clevis gap
CH_NECK = 9.3       # half width of the channel through the hub neck

BIG = 200.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl(r, z0, z1, x=0.0, y=0.0):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(r).extrude(z1 - z0))


def xhole(r, y, z, x0=-BIG / 2, x1=BIG / 2):
    return (cq.Workplane("YZ").workplane(offset=x0).center(y, z)
            .circle(r).extrude(x1 - x0))


# ---------------- main stadium plate stack ----------------
body = (cq.Workplane("XY").workplane(offset=A_BOT_BOT)
        .slot2D(2 * LC + W, W, 90).extrude(Z_TOP - A_BOT_BOT))

# lower face is higher on the +Y end
body = body.cut(box(-BIG, BIG, CAP_Y1, BIG, -BIG, B_BOT_BOT))

# gap of the -Y clevis
body = body.cut(box(-BIG, BIG, -BIG, A_STEP_Y, A_BOT_TOP, A_TOP_BOT))
body = body.cut(box(-BIG, BIG, -BIG, BODY_Y0, A_BOT_TOP, A_STEP_Z))
# gap of the +Y clevis
body = body.cut(box(-BIG, BIG, BODY_Y1, BIG, B_BOT_TOP, B_TOP_BOT))


# ---------------- raised rounded cover ----------------
# cross-section of the cover: flat crown, rounded shoulders made of a small
# side arc (radius CAP_R1, tangent to the vertical wall) and a larger arc
# (radius rm, tangent to the flat crown at CAP_XM from the wall)
def shoulder_arcs(r1, xm, h):
    # centres: c1 = (r1, 0), cm = (xm, h - rm); |c1 - cm| = rm - r1
    rm = ((xm - r1) ** 2 + h * h - r1 * r1) / (2.0 * h - 2.0 * r1)
    cmx, cmz = xm, h - rm
    dx, dz = r1 - cmx, 0.0 - cmz
    d = math.hypot(dx, dz)
    return rm, (cmx + rm * dx / d, cmz + rm * dz / d)


rmt, (tx, tz) = shoulder_arcs(CAP_R1, CAP_XM, CAP_H_TOP)
rmb, (bx, bz) = shoulder_arcs(CAP_R1, CAP_XM, CAP_H_BOT)
zt = Z_TOP
zb = A_BOT_BOT
prof = (cq.Workplane("XZ")
        .moveTo(-R, zb)
        .lineTo(-R, zt)
        .radiusArc((-R + tx, zt + tz), CAP_R1)
        .radiusArc((-R + CAP_XM, zt + CAP_H_TOP), rmt)
        .lineTo(R - CAP_XM, zt + CAP_H_TOP)
        .radiusArc((R - tx, zt + tz), rmt)
        .radiusArc((R, zt), CAP_R1)
        .lineTo(R, zb)
        .radiusArc((R - bx, zb - bz), CAP_R1)
        .radiusArc((R - CAP_XM, zb - CAP_H_BOT), rmb)
        .lineTo(-R + CAP_XM, zb - CAP_H_BOT)
        .radiusArc((-R + bx, zb - bz), rmb)
        .radiusArc((-R, zb), CAP_R1)
        .close())
cap = prof.extrude(-(CAP_Y1 - CAP_Y0)).translate((0, CAP_Y0, 0))
try:
    cap = cap.faces("<Y or >Y").edges().fillet(CAP_R_END)
except Exception:
    endr = (cq.Workplane("YZ").workplane(offset=-R)
            .center((CAP_Y0 + CAP_Y1) / 2, (zt + CAP_H_TOP + zb - CAP_H_BOT) / 2)
            .rect(CAP_Y1 - CAP_Y0, zt + CAP_H_TOP - zb + CAP_H_BOT)
            .extrude(W).edges("|X").fillet(CAP_R_END))
    cap = cap.intersect(endr)
body = body.union(cap)

# ---------------- side panel (-X) ----------------
panel = (cq.Workplane("YZ").workplane(offset=-R - PANEL_T)
         .polyline([(PANEL_Y0 + PANEL_CH0, -PANEL_Z), (PANEL_Y1 - PANEL_CH1, -PANEL_Z),
                    (PANEL_Y1, -PANEL_Z + PANEL_CH1), (PANEL_Y1, PANEL_Z - PANEL_CH1),
                    (PANEL_Y1 - PANEL_CH1, PANEL_Z), (PANEL_Y0 + PANEL_CH0, PANEL_Z),
                    (PANEL_Y0, PANEL_Z - PANEL_CH0), (PANEL_Y0, -PANEL_Z + PANEL_CH0)])
         .close().extrude(PANEL_T + 0.5))
body = body.union(panel)

# ---------------- hub of the +Y clevis ----------------
# barrel between the +Y plates, joined to the body by a straight neck
hub = (cyl(HUB_R, B_BOT_TOP - 0.01, B_TOP_BOT + 0.01, 0, LC)
       .union(box(-HUB_R, HUB_R, BODY_Y1 - 0.5, LC, B_BOT_TOP - 0.01, B_TOP_BOT + 0.01)))
body = body.union(hub)

# ---------------- channel through the body ----------------
# wide channel open to the -Y clevis gap ...
body = body.cut(box(CH_X0, CH_X1, BODY_Y0 - 1, BODY_Y1 - CH_END_T, CH_Z0, CH_Z1))
# ... continuing, narrower, through the neck into the bore of the hub
body = body.cut(box(-CH_NECK, CH_NECK, BODY_Y0 - 1, LC, CH_Z0, B_TOP_BOT))
body = body.cut(cyl(HUB_BORE, B_BOT_TOP, B_TOP_BOT, 0, LC))
# parting groove around the barrel
groove = (cq.Workplane("XY").workplane(offset=HUB_GROOVE_Z - 0.2).center(0, LC)
          .circle(HUB_R + 1.0).circle(HUB_R - 0.3).extrude(0.4))
body = body.cut(groove.cut(box(-BIG, BIG, -BIG, LC, -BIG, BIG)))

# ---------------- -Y end features ----------------
yA = -LC
# upper plate: circular recess + deeper rounded pocket + through slot
body = body.cut(cyl(A_CUP_R, Z_TOP - A_CUP_D, Z_TOP + 1, 0, yA))
pocket = (cq.Workplane("XY").workplane(offset=Z_TOP - A_POCKET_D)
          .center(-0.5, (-41.0 - 28.1) / 2).rect(17.3, 12.9).extrude(A_POCKET_D + 1))
pocket = pocket.edges("|Z").fillet(3.0)
body = body.cut(pocket)
aslot = (cq.Workplane("XY").workplane(offset=A_STEP_Z - 1)
         .center(-0.4, A_SLOT_Y0 + A_SLOT_W / 2)
         .rect(A_SLOT_L, A_SLOT_W).extrude(Z_TOP - A_STEP_Z + 2)
         .edges("|Z").fillet(A_SLOT_RC))
body = body.cut(aslot)
# stadium boss under the upper plate
boss = (cq.Workplane("XY").workplane(offset=A_TOP_BOT - 1.1)
        .center(0, -46.1).slot2D(18.4, 6.1, 0).extrude(1.2))
body = body.union(boss)
for sx in (-1, 1):
    body = body.cut(cyl(0.9, A_TOP_BOT - 2, Z_TOP + 1, sx * 6.15, -46.35))

# lower plate: bore + keyway + annular recess from below + set-screw hole
body = body.cut(cyl(A_BORE_R, A_BOT_BOT - 1, A_BOT_TOP + 1, 0, yA))
key = (box(-A_KEY_W / 2, A_KEY_W / 2, 0, 30, A_REC_TOP, A_BOT_TOP + 1)
       .rotate((0, 0, 0), (0, 0, 1), A_KEY_ANG - 90).translate((0, yA, 0)))
body = body.cut(key)
ring = (cq.Workplane("XY").workplane(offset=A_BOT_BOT - 1).center(0, yA)
        .circle(A_REC_R).circle(A_BOSS_R).extrude(1 + A_REC_TOP - A_BOT_BOT))
body = body.cut(ring)
body = body.cut(xhole(1.9, yA, -11.0))
# notch in lower plate near the body
body = body.cut(box(-BIG, BIG, A_NOTCH_Y0, A_NOTCH_Y1, -BIG, -13.9))
body = body.cut(box(A_NOTCH_X, BIG, A_NOTCH_Y0, A_NOTCH_Y1, -BIG, -10.2))
# mounting holes near the body on both plates
for sx in (-1, 1):
    body = body.cut(cyl(1.6, A_BOT_BOT - 1, Z_TOP + 1, sx * 12.6, -32.0))

# ---------------- +Y end features ----------------
yB = LC
body = body.cut(cyl(B_CUP_R, Z_TOP - 3.0, Z_TOP + 1, 0, yB))
body = body.cut(cyl(12.0, 12.4, Z_TOP + 1, 0, yB))
body = body.cut(cyl(B_CUP_R2, B_BOT_BOT - 1, B_BOT_BOT + 3.0, 0, yB))
body = body.cut(cyl(12.0, B_BOT_BOT - 1, B_BOT_BOT + 4.5, 0, yB))
body = body.cut(cyl(HUB_BORE, B_BOT_BOT - 1, B_BOT_TOP + 0.5, 0, yB))
body = body.cut(box(-5.0, 5.0, 33.0, 50.25, B_TOP_BOT - 1, BIG))
# notches at both sides of the root of the upper plate
body = body.cut(box(B_NOTCH_X, BIG, 27.4, 36.6, 12.4, BIG))
body = body.cut(box(-BIG, -B_NOTCH_X, 27.4, 36.6, 12.4, BIG))
for sx in (-1, 1):
    body = body.cut(cyl(1.6, B_BOT_BOT - 1, Z_TOP + 1, sx * 12.5, 32.0))
    body = body.cut(cyl(0.9, Z_TOP - 8, Z_TOP + 1, sx * 6.9, 42.0))

# ---------------- holes on the +X side and top ----------------
for (hy, hz) in ((-17.6, 7.25), (19.1, 6.9)):
    h = xhole(1.3, hy, hz, R - 6, R + 1)
    cs = (cq.Workplane("YZ").workplane(offset=R - 1.2).center(hy, hz)
          .circle(1.3).workplane(offset=1.3).circle(2.5).loft())
    body = body.cut(h).cut(cs)
body = body.cut(cyl(0.8, Z_TOP, Z_TOP + 10, -8.4, 19.0))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
